import cadquery as cq

# O-ring / torus lying flat in the XY plane, centred on the origin
outer_diameter = 50.0      # overall outside diameter (mm)
cross_section_d = 10.0     # cord (tube) diameter (mm)
seam_angle = 135.0         # where the meridian seam sits (deg about Z)

minor_r = cross_section_d / 2.0                 # tube radius
major_r = outer_diameter / 2.0 - minor_r        # centre-line radius
inner_diameter = outer_diameter - 2 * cross_section_d

# Circular cord section in the vertical plane y = 0, centred at x = major_r.
# The plane's local x points straight down (-Z) so the circle's start seam
# lies on the underside of the cord; local y is then +X.
section_plane = cq.Plane(origin=(major_r, 0, 0), xDir=(0, 0, -1), normal=(0, -1, 0))
section = cq.Workplane(section_plane).circle(minor_r)

# Revolve a full turn about the global Z axis.  In the section plane's local
# coordinates that axis passes through (0, -major_r) along local -x.
ring = section.revolve(360, (0, -major_r, 0), (-1, -major_r, 0))

# Turn the meridian seam away from the main viewing direction
result = ring.rotate((0, 0, 0), (0, 0, 1), seam_angle)

VIEW = {"azimuth": 45, "elevation": 26}
